import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
PLATE_T = 3.8          # nominal plate thickness
FACET_STEP = 0.12      # height step between neighbouring top facets
POST_D = 11.7          # standoff diameter
POST_H = 13.1          # standard standoff height above plate
POST_H_SHORT = 10.6    # short standoffs (carry taller pins)
NECK_D = 5.8           # pin neck diameter
HEAD_D = 7.0           # pin head diameter
HEAD_H = 1.0           # pin head height
PIN_H = 3.5            # standard pin height
PIN_H_TALL = 6.0       # tall pin height
PIN_CHAMFER = 0.35
SLOT_W = 1.0
SLOT_D = 0.9
CORNER_R = 4.5         # convex outline corner rounding
CONCAVE_R = 0.8        # concave outline corner rounding
CB_D = 11.6            # underside recess at each post (outer step)
CB_DEPTH = 0.25
CB2_D = 8.2            # underside recess at each post (inner step)
CB2_DEPTH = 0.5
GROOVE_W = 0.35        # underside crease grooves
GROOVE_D = 0.12
SEAM_ANG = 100.0       # cylinder seams turned towards +Y (hidden in front views)

# reference frame: outline digitised on a 1 mm grid (top view, y pointing down)
OX, OY = 130.0, 390.0


def P(x, y):
    """digitised top-view coordinates (y down) -> model XY (mm)"""
    return (x - OX, OY - y)


# ---------------- posts ----------------
# name: (x, y, short?, slotted?, slot angle deg)
POSTS = {
    "P1": (23.75, 317.5, False, False, 0),
    "P2": (50.9, 385.1, False, False, 0),
    "P3": (137.1, 278.7, False, True, -15),
    "P4": (90.4, 323.2, False, True, 45),
    "P5": (162.8, 325.9, False, True, 30),
    "P6": (116.4, 383.7, False, False, 0),
    "P7": (233.2, 319.1, True, False, 0),
    "P8": (207.7, 412.9, True, True, 0),
    "P9": (151.3, 463.6, False, True, 0),
    "P10": (236.5, 463.1, False, True, 0),
    "P11": (206.5, 499.2, False, False, 0),
}
# posts bulging out of a straight edge: plate ear = circle fused to outline
EAR_POSTS = {"P3": 7.8, "P6": 7.0}


def pc(n):
    return (POSTS[n][0], POSTS[n][1])


# ---------------- plate outline ----------------
# plain tuples are corners; ("arc", post, r) wraps the corner round a post
# with a radius-r arc tangent to both neighbouring edges.
V1 = (222.9, 382.6)
V2 = (166.9, 401.5)
V3 = (215.6, 434.6)
OUTLINE = [
    (35.6, 278.7),
    (92.7, 283.1),
    (92.7, 277.6),
    (97.0, 273.9),
    (131.0, 279.0),
    (137.1, 278.7),
    (141.6, 272.3),
    (177.3, 280.4),
    (177.3, 288.3),
    (211.2, 297.0),
    (211.4, 306.2),
    ("arc", "P7", 7.0),
    V1,
    V3,
    ("arc", "P10", 9.4),
    ("arc", "P11", 8.1),
    (176.6, 485.5),
    ("arc", "P9", 7.6),
    (166.9, 413.8),
    V2,
    (140.2, 393.3),
    (138.2, 386.6),
    (123.0, 383.6),
    (116.4, 383.7),
    (112.0, 389.8),
    (94.5, 386.6),
    (91.7, 386.8),
    (90.8, 395.3),
    ("arc", "P2", 7.2),
    (45.1, 359.6),
    (18.0, 357.0),
    (14.6, 351.0),
    ("arc", "P1", 7.6),
    (31.5, 309.4),
]

# ---------------- top facets (panels) ----------------
# polygons may overshoot the outline; they are clipped to it.
# value = facet height in FACET_STEP units relative to nominal top.
P1, P2, P3, P4, P5, P6 = (pc(n) for n in ("P1", "P2", "P3", "P4", "P5", "P6"))
P7, P8, P9, P10, P11 = (pc(n) for n in ("P7", "P8", "P9", "P10", "P11"))
PANELS = [
    # upper section
    ([(0, 250), (93.2, 250), (92.9, 276), P4, P6, (116.4, 425), (0, 425)], 0),   # A
    ([(93.2, 250), (137.1, 250), P3, P4, (92.9, 276)], 2),                       # B1
    ([P4, P3, P5], 1),                                                           # B2
    ([P4, P5, P6], -1),                                                          # B3
    ([P3, (137.1, 250), (262, 250), (262, 378), V1, V2, (160, 420),
      (116.4, 425), P6, P5], 3),                                                 # C
    ([(211.1, 305.8), (214, 298), (248, 306), P7], 4),                           # S1
    ([P7, (252, 318), (241, 349), (231.9, 348.8)], 4),                           # S2
    ([P1, (8, 311), (8, 352), (14.4, 350.5)], 1),                                # S3
    # lower section
    ([V2, V1, P8], 2),                                                           # L1
    ([V1, (236, 380), (231, 437), V3, P8], 3),                                   # L1b
    ([V2, P8, V3, P9, (136, 467), (150, 405)], 1),                               # L2
    ([V3, P9, (134, 472), (205, 522), (256, 470), (247, 450)], 0),               # L3
    ([(P11[0] + 3.0, P11[1] - 4.0), (P10[0] - 4.0, P10[1] + 3.2),
      (262, 470), (212, 525)], 2),                                               # L4
    ([(P11[0] + 3.0, P11[1] - 4.0), (P10[0] - 4.0, P10[1] + 3.2),
      (P11[0] + 7.3, P11[1] + 0.3)], 3),                                         # L4a
]

# bold crease lines: a narrow intermediate strip laid on the lower side
BOLD_W = 0.6
_cen = lambda *ps: (sum(p[0] for p in ps) / len(ps), sum(p[1] for p in ps) / len(ps))
BOLD_LINES = [
    # (start, end, point inside lower panel, strip level)
    ((93.2, 262.0), P4, (50.0, 330.0), 1),                     # A | B1
    (P3, P5, _cen(P4, P3, P5), 2),                             # B2 | C
    (P4, P5, _cen(P4, P5, P6), 0),                             # B3 | B2
    (P5, P6, _cen(P4, P5, P6), 0),                             # B3 | C
    ((P11[0] + 3.0, P11[1] - 4.0), (P10[0] - 4.0, P10[1] + 3.2),
     (190.0, 470.0), 1),                                       # L3 | L4
]
for a, b, inside, lvl in BOLD_LINES:
    dx, dy = b[0] - a[0], b[1] - a[1]
    ln = (dx * dx + dy * dy) ** 0.5
    nx, ny = -dy / ln, dx / ln
    if (inside[0] - a[0]) * nx + (inside[1] - a[1]) * ny < 0:
        nx, ny = -nx, -ny
    PANELS.append(([a, b, (b[0] + nx * BOLD_W, b[1] + ny * BOLD_W),
                    (a[0] + nx * BOLD_W, a[1] + ny * BOLD_W)], lvl))
BASE_DROP = 2 * FACET_STEP   # base plate top below nominal (under the facets)


# ---------------- outline construction helpers ----------------
def _sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def _cross(a, b):
    return a[0] * b[1] - a[1] * b[0]


def _tangent_point(ext, c, r, sgn, incoming):
    """tangent point on circle (c, r) seen from external point ext.
    sgn = +1 for a CCW outline (circle must lie left of the edge)."""
    d = _sub(ext, c)
    dist = math.hypot(*d)
    base = math.atan2(d[1], d[0])
    alpha = math.acos(min(1.0, r / dist))
    best = None
    for s in (1.0, -1.0):
        a = base + s * alpha
        t = (c[0] + r * math.cos(a), c[1] + r * math.sin(a))
        if incoming:      # edge ext -> t
            cr = _cross(_sub(t, ext), _sub(c, ext))
        else:             # edge t -> ext
            cr = _cross(_sub(ext, t), _sub(c, t))
        if cr * sgn > 0:
            best = t
    return best


def _common_tangent(c1, r1, c2, r2, sgn):
    """outer tangent leaving circle 1 and arriving at circle 2, both circles
    on the interior side of the outline; returns (t1, t2)."""
    dx, dy = c2[0] - c1[0], c2[1] - c1[1]
    D = math.hypot(dx, dy)
    ux, uy = dx / D, dy / D
    px, py = -uy, ux                      # left normal of the travel direction
    b = math.acos((r2 - r1) / D)
    sb = math.sin(b) * sgn
    nx, ny = math.cos(b) * ux + sb * px, math.cos(b) * uy + sb * py
    return ((c1[0] - r1 * nx, c1[1] - r1 * ny),
            (c2[0] - r2 * nx, c2[1] - r2 * ny))


def build_outline_wire(items):
    # model-space items
    mitems = []
    for it in items:
        if isinstance(it[0], str):
            mitems.append(("arc", P(*pc(it[1])), it[2]))
        else:
            mitems.append(("pt", P(*it)))
    # orientation from the control polygon
    ctrl = [m[1] for m in mitems]
    area = 0.0
    for i in range(len(ctrl)):
        a, b = ctrl[i], ctrl[i - 1]
        area += _cross(b, a)
    sgn = 1.0 if area > 0 else -1.0
    n = len(mitems)
    # entry / exit points of every item
    t_in = [None] * n
    t_out = [None] * n
    for i, m in enumerate(mitems):
        if m[0] == "pt":
            t_in[i] = t_out[i] = m[1]
    for i, m in enumerate(mitems):
        if m[0] != "arc":
            continue
        c, r = m[1], m[2]
        prv = mitems[i - 1]
        nxt = mitems[(i + 1) % n]
        if prv[0] == "pt":
            t_in[i] = _tangent_point(prv[1], c, r, sgn, True)
        if nxt[0] == "pt":
            t_out[i] = _tangent_point(nxt[1], c, r, sgn, False)
        else:
            t_out[i], t_in[(i + 1) % n] = _common_tangent(c, r, nxt[1], nxt[2], sgn)
    # edges
    edges = []
    for i, m in enumerate(mitems):
        if m[0] == "arc":
            c, r = m[1], m[2]
            t1, t2 = t_in[i], t_out[i]
            a1 = math.atan2(t1[1] - c[1], t1[0] - c[0])
            a2 = math.atan2(t2[1] - c[1], t2[0] - c[0])
            if sgn > 0:
                while a2 < a1:
                    a2 += 2 * math.pi
            else:
                while a2 > a1:
                    a2 -= 2 * math.pi
            am = 0.5 * (a1 + a2)
            mid = (c[0] + r * math.cos(am), c[1] + r * math.sin(am))
            edges.append(cq.Edge.makeThreePointArc(
                cq.Vector(*t1, 0), cq.Vector(*mid, 0), cq.Vector(*t2, 0)))
        a = t_out[i]
        b = t_in[(i + 1) % n]
        if math.hypot(a[0] - b[0], a[1] - b[1]) > 1e-6:
            edges.append(cq.Edge.makeLine(cq.Vector(*a, 0), cq.Vector(*b, 0)))
    return cq.Wire.assembleEdges(edges)


# --- outline face: belts round corner posts + fused ears, corners rounded ---
wire0 = build_outline_wire(OUTLINE)
blank = cq.Workplane("XY").add(
    cq.Solid.extrudeLinear(cq.Face.makeFromWires(wire0), cq.Vector(0, 0, 1.0)))
for n, r in EAR_POSTS.items():
    blank = blank.union(
        cq.Workplane("XY").center(*P(*pc(n))).circle(r).extrude(1.0))
outer = blank.faces(">Z").val().outerWire()
w = outer.offset2D(-CORNER_R, "arc")[0].offset2D(CORNER_R, "arc")[0]
w = w.offset2D(CONCAVE_R, "arc")[0].offset2D(-CONCAVE_R, "arc")[0]
w = w.translate(cq.Vector(0, 0, -1.0))          # back to z = 0
outline_face = cq.Face.makeFromWires(w)


def prism(face, z0, h):
    return cq.Solid.extrudeLinear(face.translate(cq.Vector(0, 0, z0)),
                                  cq.Vector(0, 0, h))


base_top = PLATE_T - BASE_DROP
plate = cq.Workplane("XY").add(prism(outline_face, 0.0, base_top))
clip = prism(outline_face, base_top - 0.1, 5.0)

# --- faceted top: each panel clipped to the outline ---
for poly, lvl in PANELS:
    ztop = PLATE_T + lvl * FACET_STEP
    h = ztop - (base_top - 0.05)
    pp = [P(x, y) for (x, y) in poly]
    panel = (cq.Workplane("XY").workplane(offset=base_top - 0.05)
             .polyline(pp).close().extrude(h))
    panel = panel.intersect(cq.Workplane("XY").add(clip))
    plate = plate.union(panel)


# ---------------- standoffs with pins ----------------
def make_post(short, slotted, ang):
    """standoff + pin built at the origin, seam turned to SEAM_ANG"""
    h = POST_H_SHORT if short else POST_H
    ph = PIN_H_TALL if short else PIN_H
    z0 = base_top
    body = (cq.Workplane("XY").workplane(offset=z0)
            .circle(POST_D / 2).extrude(PLATE_T + h - z0))
    ztop = PLATE_T + h
    neck = (cq.Workplane("XY").workplane(offset=ztop)
            .circle(NECK_D / 2).extrude(ph - HEAD_H))
    head = (cq.Workplane("XY").workplane(offset=ztop + ph - HEAD_H)
            .circle(HEAD_D / 2).extrude(HEAD_H)
            .faces(">Z").edges().chamfer(PIN_CHAMFER))
    pin = neck.union(head)
    post = body.union(pin).rotate((0, 0, 0), (0, 0, 1), SEAM_ANG)
    if slotted:
        top = ztop + ph
        slot = (cq.Workplane("XY").workplane(offset=top - SLOT_D)
                .transformed(rotate=(0, 0, ang))
                .rect(HEAD_D * 1.5, SLOT_W).extrude(SLOT_D + 1))
        post = post.cut(slot)
    return post


for n, (x, y, short, slotted, ang) in POSTS.items():
    cx, cy = P(x, y)
    plate = plate.union(make_post(short, slotted, ang).translate((cx, cy, 0)))

# ---------------- underside stepped recesses ----------------
for n in POSTS:
    cx, cy = P(*pc(n))
    cb = (cq.Workplane("XY").circle(CB_D / 2).extrude(CB_DEPTH)
          .union(cq.Workplane("XY").circle(CB2_D / 2).extrude(CB2_DEPTH))
          .rotate((0, 0, 0), (0, 0, 1), SEAM_ANG).translate((cx, cy, 0)))
    plate = plate.cut(cb)

# ---------------- underside crease lines (shallow grooves) ----------------
UNDER_CREASES = [
    (V3, (176.6, 485.5)),
    (V2, P8),
    ((139.3, 390.0), P5),
]
for a, b in UNDER_CREASES:
    (ax, ay), (bx, by) = P(*a), P(*b)
    L = math.hypot(bx - ax, by - ay)
    ang = math.degrees(math.atan2(by - ay, bx - ax))
    g = (cq.Workplane("XY").workplane(offset=-1.0)
         .center((ax + bx) / 2, (ay + by) / 2)
         .transformed(rotate=(0, 0, ang))
         .rect(L, GROOVE_W).extrude(1.0 + GROOVE_D))
    plate = plate.cut(g)

result = plate
